import math
import cadquery as cq

# ---------------------------------------------------------------------------
# Hexagonal robot body: hex top plate, three servo housings (two servos each)
# on alternating sides, side wings, bottom Y-frame, top-side hardware.
# ---------------------------------------------------------------------------

# ---- driving dimensions (mm) ----
R = 60.0                              # plate circumradius (vertices 30,90,..)
A = R * math.cos(math.radians(30))    # plate apothem (flat edges 0,60,..)
T = 3.5                               # plate thickness
H = 55.8                              # bottom (z=0) to plate top
ZT = H                                # plate top
ZP = H - T                            # plate underside
CORNER_R = 3.0                        # plan-view corner rounding of plate
EDGE_R = 1.3                          # top edge rounding of plate

SERVO_AXES = [0.0, 120.0, 240.0]      # directions of servo faces
PLAIN_AXES = [60.0, 180.0, 300.0]     # directions of open faces

CORE_HW = 20.0                        # half width of servo bodies (core)
HW = 22.4                             # half width of housing frame
FRAME_U0 = 30.0                       # inner end of housing frame
XF = A - 0.8                          # housing front face
COVER_T = 1.5                         # servo cover thickness
Z_CORE_BOT = 7.6                      # underside of servo bodies / core
SERVO_YC = 10.85                      # servo centre offset from housing axis
SERVO_HW = 9.6                        # half width of servo cover
SHAFT_Z = ZT - 37.1                   # output shaft height
ARCH_R = 6.15                         # radius of the cover's top hump
ARCH_H = 3.4                          # height of the hump
BOSS_R = 6.9                          # decagon boss circumradius
SPLINE_R = 3.3                        # output spline radius
SPLINE_TIP = A + 5.4                  # radial position of spline tip

WING_P = 22.4                         # inner face offset of wings
WING_T = 2.0                          # wing thickness
WING_U0 = 29.5                        # inner end of wing
WING_U1 = 50.3                        # outer end of wing at top
WING_U1B = 50.3                       # outer end of wing at bottom
WING_RO = 4.0                         # outer bottom corner radius
WING_RI = 3.5                         # inner bottom corner radius
WING_ZB = 0.3                         # wing bottom

NUT_AF = 5.0                          # M3 nut across flats
NUT_H = 1.5
PIN_TOP = ZT + 10.0                   # tip of header pins
HDR_U = 0.337 * A                     # radial position of pin headers
PIN_R = 1.05                          # round header pins (touching)
PIN_PITCH = 2.2
HDR_T = 3.2                           # header housing thickness
HDR_L = 7.0                           # header housing length
HDR_H = 3.4                           # header housing height
SLOT_U = 0.81 * A                     # radial position of connector slots

LUG_U = 45.6                          # radial position of mounting lugs
LUG_Z = 3.1                           # lug centre height
LUG_R = 3.0
CELL_ZB = 2.4                         # underside of the lug cells

YF_Z0 = 0.6                           # underside of Y-frame
YF_T = 2.0                            # Y-frame plate thickness
YF_W = 5.0                            # Y-frame arm width
YF_RIB_T = 2.5                        # rib thickness on each arm
YF_LEN = LUG_U - 6.0                  # arm length from centre


def rot(shape, ang):
    return shape.rotate((0, 0, 0), (0, 0, 1), ang)


def hexnut_z(x, y, z0, af=NUT_AF, h=NUT_H, ang=0.0):
    """Hex nut standing on z0 with a rounded screw end on top."""
    d = af / math.cos(math.radians(30))
    n = (cq.Workplane("XY").workplane(offset=z0)
         .polygon(6, d).extrude(h)
         .edges(">Z").chamfer(0.3))
    tip = (cq.Workplane("XY").workplane(offset=z0 + h)
           .circle(1.35).extrude(0.7).faces(">Z").edges().fillet(0.4))
    n = n.union(tip)
    n = n.rotate((0, 0, 0), (0, 0, 1), ang)
    return n.translate((x, y, 0))


# ---------------------------------------------------------------------------
# top plate
# ---------------------------------------------------------------------------
hex_pts = [(R * math.cos(math.radians(30 + 60 * i)),
            R * math.sin(math.radians(30 + 60 * i))) for i in range(6)]
plate = (cq.Workplane("XY").workplane(offset=ZP)
         .polyline(hex_pts).close().extrude(T)
         .edges("|Z").fillet(CORNER_R)
         .faces(">Z").edges().fillet(EDGE_R))

# through holes on the open-face axes
for ang in PLAIN_AXES:
    c, s = math.cos(math.radians(ang)), math.sin(math.radians(ang))
    r0 = 0.91 * A
    plate = plate.cut(cq.Workplane("XY").workplane(offset=ZP - 1)
                      .center(r0 * c, r0 * s).circle(1.6).extrude(T + 2))

# slots for the servo connector strips
for ang in SERVO_AXES:
    slot = (cq.Workplane("XY").workplane(offset=ZP - 1)
            .center(SLOT_U + 0.4, 0).rect(4.4, 43.5).extrude(T + 2))
    plate = plate.cut(rot(slot, ang))

# shallow scribed lines on the top face (outline of the cover sheet)
GROOVE_W = 0.35
GROOVE_D = 0.2
GROOVES = [
    ((-0.93, -0.51), (-0.79, -0.285)), ((-0.79, -0.285), (-0.79, 0.285)),
    ((-0.79, 0.285), (-0.91, 0.0)), ((-0.91, 0.0), (-0.93, -0.51)),
    ((0.024, 1.06), (0.149, 0.827)), ((0.149, 0.827), (0.149, -0.827)),
    ((0.149, -0.827), (0.024, -1.06)),
    ((0.149, 0.827), (-0.04, 0.91)), ((0.149, -0.827), (-0.04, -0.91)),
]
for (p0, p1) in GROOVES:
    x0, y0 = p0[0] * A, p0[1] * A
    x1, y1 = p1[0] * A, p1[1] * A
    ln = math.hypot(x1 - x0, y1 - y0)
    ang = math.degrees(math.atan2(y1 - y0, x1 - x0))
    g = (cq.Workplane("XY").workplane(offset=ZT - GROOVE_D)
         .rect(ln, GROOVE_W).extrude(1.0)
         .rotate((0, 0, 0), (0, 0, 1), ang)
         .translate(((x0 + x1) / 2.0, (y0 + y1) / 2.0, 0)))
    plate = plate.cut(g)

body = plate


# ---------------------------------------------------------------------------
# servo housings / central core
# ---------------------------------------------------------------------------
def housing():
    hgt = ZP - Z_CORE_BOT
    core = (cq.Workplane("XY").workplane(offset=Z_CORE_BOT)
            .center(FRAME_U0 / 2.0, 0).rect(FRAME_U0 + 1.0, 2 * CORE_HW)
            .extrude(hgt))
    frame = (cq.Workplane("XY").workplane(offset=Z_CORE_BOT)
             .center((FRAME_U0 + XF) / 2.0, 0).rect(XF - FRAME_U0, 2 * HW)
             .extrude(hgt))
    h = core.union(frame)
    # shallow parting groove between the two servos
    h = h.cut(cq.Workplane("YZ").workplane(offset=XF - 0.6)
              .center(0, (ZP + Z_CORE_BOT) / 2.0)
              .rect(0.8, hgt + 2).extrude(1.0))
    return h


def servo_face(yc):
    """Servo top cover with label recess, decagon boss and output spline."""
    x0 = XF
    cz = SHAFT_Z
    top = ZT - 11.1
    sk = (cq.Sketch()
          .push([(yc, (top + cz) / 2.0)])
          .rect(2 * SERVO_HW, top - cz)
          .reset()
          .push([(yc, cz)]).regularPolygon(SERVO_HW / math.cos(math.pi / 10), 10)
          .reset()
          .push([(yc, top - ARCH_R * math.cos(math.pi / 10) + ARCH_H)])
          .regularPolygon(ARCH_R, 10)
          .clean())
    cover = (cq.Workplane("YZ").workplane(offset=x0).placeSketch(sk)
             .extrude(COVER_T))
    # flat bottom of the cover
    cover = cover.cut(cq.Workplane("YZ").workplane(offset=x0 - 1)
                      .center(yc, ZT - 47.1 - 5.0)
                      .rect(30, 10).extrude(5))
    xc = x0 + COVER_T
    # label recess (leaves a raised border)
    cover = cover.cut(cq.Workplane("YZ").workplane(offset=xc - 0.5)
                      .center(yc, ZT - 18.2).rect(16.4, 10.8).extrude(1.0))
    # small notch under the label
    cover = cover.cut(cq.Workplane("YZ").workplane(offset=xc - 0.5)
                      .center(yc, ZT - 24.5).circle(1.4).extrude(1.0))
    # two-tier decagon boss
    boss = (cq.Workplane("YZ").workplane(offset=xc)
            .center(yc, cz).polygon(10, 2 * BOSS_R).extrude(0.9))
    boss2 = (cq.Workplane("YZ").workplane(offset=xc + 0.9)
             .center(yc, cz).polygon(10, 2 * (BOSS_R - 1.2)).extrude(0.5))
    x_sp = xc + 1.4
    spline = (cq.Workplane("YZ").workplane(offset=x_sp)
              .center(yc, cz).circle(SPLINE_R).extrude(SPLINE_TIP - x_sp))
    spline = spline.faces(">X").edges().chamfer(0.35)
    spline = spline.cut(cq.Workplane("YZ").workplane(offset=SPLINE_TIP - 1.2)
                        .center(yc, cz).circle(1.1).extrude(2))
    return cover.union(boss).union(boss2).union(spline)


def bottom_tabs():
    """Lug cells under the servo faces: back bar, dividers, lugs, nuts."""
    top = Z_CORE_BOT + 0.5
    bar = (cq.Workplane("XY").workplane(offset=1.2)
           .center(LUG_U - 5.5, 0).rect(6.0, 2 * HW).extrude(top - 1.2))
    # outer cheeks and dividers of the cells
    for y in (-HW + 0.7, HW - 0.7):
        d = (cq.Workplane("XY").workplane(offset=CELL_ZB)
             .center((LUG_U - 3.0 + XF) / 2.0, y)
             .rect(XF - LUG_U + 3.0, 1.4).extrude(top - CELL_ZB))
        bar = bar.union(d)
    for y in (-SERVO_YC, 0.0, SERVO_YC):
        d = (cq.Workplane("YZ").workplane(offset=LUG_U - 3.0)
             .polyline([(y - 0.6, top), (y + 0.6, top), (y + 0.6, CELL_ZB + 2.0),
                        (y - 0.6, CELL_ZB + 2.0)]).close().extrude(5.5))
        d = d.cut(cq.Workplane("XZ", origin=(0, y + 1, 0))
                  .polyline([(LUG_U + 2.5, top + 1), (LUG_U + 2.5, CELL_ZB + 1.0),
                             (LUG_U - 0.5, CELL_ZB + 1.0)]).close().extrude(2.0))
        bar = bar.union(d)
    for y in (-16.3, -5.6, 5.6, 16.3):
        lug = (cq.Workplane("YZ").workplane(offset=LUG_U - 3.0)
               .center(y, LUG_Z).circle(LUG_R).extrude(3.0))
        nut = (cq.Workplane("YZ").workplane(offset=LUG_U)
               .center(y, LUG_Z).circle(LUG_R - 0.3).extrude(1.4)
               .faces(">X").edges().chamfer(0.3))
        nut = nut.cut(cq.Workplane("YZ").workplane(offset=LUG_U + 0.6)
                      .center(y, LUG_Z).polygon(6, 2.9).extrude(2))
        inut = (cq.Workplane("YZ").workplane(offset=LUG_U - 9.7)
                .center(y, 4.2).polygon(6, 5.4).extrude(1.2))
        inut = inut.cut(cq.Workplane("YZ").workplane(offset=LUG_U - 10.7)
                        .center(y, 4.2).circle(1.3).extrude(0.9))
        bar = bar.union(lug).union(nut).union(inut)
    return bar


def wing(side):
    """Side plate along the housing flank, bolted under the plate."""
    zt = ZP
    pts = [(WING_U0, zt), (WING_U1, zt), (WING_U1B, WING_ZB),
           (WING_U0, WING_ZB)]
    # XZ workplane extrudes along -Y; build on +side then mirror if needed
    w = (cq.Workplane("XZ", origin=(0, WING_P + WING_T, 0))
         .polyline(pts).close().extrude(WING_T))
    w = w.edges("|Y").edges("<Z").edges(">X").fillet(WING_RO)
    w = w.edges("|Y").edges("<Z").edges("<X").fillet(WING_RI)
    # bevel: outer face cut back from the crease line to the outer edge
    yo = WING_P + WING_T + 0.01
    yi = WING_P + 0.45
    cu0, cu1 = 41.7, 49.0          # crease position at top / bottom
    ue = WING_U1 + 4.0
    k = (yo - yi) / (ue - cu0)     # constant slope -> planar bevel
    yb = yo - k * (ue - cu1)
    bevel = (cq.Workplane("XY")
             .polyline([(cu1, yo), (ue, yb), (ue, yo + 2),
                        (cu1 - 0.01, yo + 2)]).close()
             .workplane(offset=zt + 0.5)
             .polyline([(cu0, yo), (ue, yi), (ue, yo + 2),
                        (cu0 - 0.01, yo + 2)]).close()
             .loft(ruled=True))
    w = w.cut(bevel)
    # flange under the plate with gusset and screw heads
    fl = (cq.Workplane("XY").workplane(offset=ZP - 1.6)
          .center((WING_U0 + 2.0 + WING_U1 - 1.0) / 2.0,
                  WING_P + WING_T + 2.8)
          .rect(WING_U1 - WING_U0 - 3.0, 5.6).extrude(1.6))
    gus = (cq.Workplane("YZ").workplane(offset=40.3)
           .polyline([(WING_P + WING_T - 0.1, ZP - 6.5),
                      (WING_P + WING_T + 5.0, ZP),
                      (WING_P + WING_T - 0.1, ZP)]).close().extrude(1.6))
    w = w.union(fl).union(gus)
    for u in (33.4, 47.0):
        head = (cq.Workplane("XY").workplane(offset=ZP - 2.8)
                .center(u, 28.6).circle(2.4).extrude(1.3))
        w = w.union(head)
    if side < 0:
        w = w.mirror("XZ")
    return w


for ang in SERVO_AXES:
    h = housing()
    for yc in (-SERVO_YC, SERVO_YC):
        h = h.union(servo_face(yc))
    h = h.union(bottom_tabs())
    h = h.union(wing(1)).union(wing(-1))
    body = body.union(rot(h, ang))

# ---------------------------------------------------------------------------
# bottom Y-frame: flat Y plate with filleted junctions plus a rib per arm
# ---------------------------------------------------------------------------

yframe = (cq.Workplane("XY").workplane(offset=YF_Z0)
          .circle(6.0).extrude(YF_T))
for ang in SERVO_AXES:
    arm = (cq.Workplane("XY").workplane(offset=YF_Z0)
           .center(YF_LEN / 2.0, 0).rect(YF_LEN, YF_W).extrude(YF_T))
    yframe = yframe.union(rot(arm, ang))
yframe = (yframe.edges("|Z")
          .edges(cq.selectors.BoxSelector((-8, -8, -1), (8, 8, 10)))
          .fillet(3.0))
yframe = yframe.cut(cq.Workplane("XY").circle(1.6).extrude(10))
for ang in SERVO_AXES:
    rib = (cq.Workplane("XY").workplane(offset=YF_Z0 + YF_T)
           .center((7.0 + YF_LEN) / 2.0, 0)
           .rect(YF_LEN - 7.0, YF_RIB_T).extrude(Z_CORE_BOT - YF_Z0 - YF_T + 0.2))
    yframe = yframe.union(rot(rib, ang))
body = body.union(yframe)

# ---------------------------------------------------------------------------
# top side hardware: nuts, pin headers, connector strips
# ---------------------------------------------------------------------------
nut_pts = []
for ang in PLAIN_AXES:
    for (u, v) in ((0.79 * A, 0.285 * A), (0.79 * A, -0.285 * A),
                   (0.93 * A, 0.51 * A), (0.93 * A, -0.51 * A)):
        c, s = math.cos(math.radians(ang)), math.sin(math.radians(ang))
        nut_pts.append((u * c - v * s, u * s + v * c))
for (x, y) in nut_pts:
    body = body.union(hexnut_z(x, y, ZT, ang=15.0))


def pin_header():
    base = (cq.Workplane("XY").workplane(offset=ZT)
            .rect(HDR_T, HDR_L).extrude(HDR_H, taper=8)
            .faces(">Z").edges().fillet(0.4))
    for k in (-1, 0, 1):
        pin = (cq.Workplane("XY").workplane(offset=ZT + HDR_H - 0.4)
               .center(0, PIN_PITCH * k).circle(PIN_R)
               .extrude(PIN_TOP - ZT - HDR_H + 0.4)
               .faces(">Z").edges().fillet(0.5))
        base = base.union(pin)
    return base


for ang in SERVO_AXES:
    for v in (-SERVO_YC, SERVO_YC):
        body = body.union(rot(pin_header().translate((HDR_U, v, 0)), ang))


def conn_strip():
    """Servo plug housings sticking up through the slot in the plate."""
    s = None
    for sg in (1.0, -1.0):
        blocks = [(16.0, 21.6, 2.6), (6.6, 14.8, 2.9), (1.2, 4.9, 2.6)]
        for (y0, y1, hh) in blocks:
            b = (cq.Workplane("XY").workplane(offset=ZP - 0.5)
                 .center(SLOT_U, sg * (y0 + y1) / 2.0).rect(3.0, y1 - y0)
                 .extrude(T + 0.5 + hh))
            b = b.faces(">Z").edges(">X").chamfer(0.6)
            s = b if s is None else s.union(b)
        # latch bump on the long block, facing the plate edge
        st = (cq.Workplane("XY").workplane(offset=ZP - 0.5)
              .center(SLOT_U + 1.9, sg * 11.0).rect(1.2, 3.4)
              .extrude(T + 0.5 + 2.0))
        s = s.union(st)
    return s


for ang in SERVO_AXES:
    body = body.union(rot(conn_strip(), ang))

result = body
